import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 72.0          # overall width  (X)
D = 20.0          # overall depth  (Y)
H = 100.0         # overall height (Z), open at the top
T = 2.0           # wall thickness
T_FLOOR = 2.0     # floor thickness

R_VERT = 1.5      # outer vertical edge fillet
R_BOT = 1.0       # outer bottom edge fillet
R_TOP = 1.2       # outer top rim edge fillet

LID_DROP = 3.8    # internal features stop this far below the rim

# card guides (PCB slot) on both side walls, near the back wall
RIB_PROTRUDE = 2.0
RIB1_T = 1.6      # rib touching the back wall
SLOT_W = 1.3      # PCB slot width
RIB2_T = 1.6      # second rib

# screw bosses in the two front inner corners
BOSS_S = 6.7
BOSS_HOLE_D = 2.9
BOSS_HOLE_DEPTH = 12.0

# cross bridge along X, centred in Y: a plate carried on two end legs,
# standing clear of the floor hole, with a small clearance to the side walls
BAR_T = 2.0
BAR_Z0 = 8.0      # underside of the bridge plate
BAR_Z1 = 18.0     # top of the bridge plate
BAR_GAP = 0.3     # clearance to the side walls
LEG_W = 3.0       # width (X) of each end leg

# hole through the floor, centred
FLOOR_HOLE_D = 7.0
FLOOR_HOLE_R_EDGE = 1.0   # rounded outer edge of the floor hole

# round pads on the back face
PAD_D = 8.5
PAD_H = 0.5
PAD_X = W / 2 - 9.0
PAD_Z_OFF = 13.0

# ---------------- derived ----------------
XI = W / 2 - T        # inner half width
YI = D / 2 - T        # inner half depth
Z_TOP_FEAT = H - LID_DROP

# ---------------- outer body ----------------
body = (
    cq.Workplane("XY")
    .box(W, D, H, centered=(True, True, False))
    .edges("|Z").fillet(R_VERT)
    .faces("<Z").edges().fillet(R_BOT)
    .faces(">Z").edges().fillet(R_TOP)
)

# cavity
cavity = (
    cq.Workplane("XY")
    .box(2 * XI, 2 * YI, H, centered=(True, True, False))
    .translate((0, 0, T_FLOOR))
)
body = body.cut(cavity)

# floor hole with a rounded outer edge
floor_hole = (
    cq.Workplane("XY")
    .circle(FLOOR_HOLE_D / 2)
    .extrude(T_FLOOR + 0.2)
    .translate((0, 0, -0.1))
)
body = body.cut(floor_hole)
body = body.edges(
    cq.selectors.NearestToPointSelector((0, FLOOR_HOLE_D / 2, 0))
).fillet(FLOOR_HOLE_R_EDGE)


def block(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY")
        .box(abs(x1 - x0), abs(y1 - y0), abs(z1 - z0), centered=False)
        .translate((min(x0, x1), min(y0, y1), min(z0, z1)))
    )


# card guides
for sx in (-1, 1):
    xw = sx * XI
    xr = sx * (XI - RIB_PROTRUDE)
    r1 = block(xw, xr, YI - RIB1_T, YI, T_FLOOR - 0.01, Z_TOP_FEAT)
    y2a = YI - RIB1_T - SLOT_W
    r2 = block(xw, xr, y2a - RIB2_T, y2a, T_FLOOR - 0.01, Z_TOP_FEAT)
    body = body.union(r1).union(r2)

# front corner screw bosses
for sx in (-1, 1):
    xw = sx * XI
    xb = sx * (XI - BOSS_S)
    b = block(xw, xb, -YI, -YI + BOSS_S, T_FLOOR - 0.01, Z_TOP_FEAT)
    body = body.union(b)
    hx = sx * (XI - BOSS_S / 2)
    hy = -YI + BOSS_S / 2
    hole = (
        cq.Workplane("XY")
        .circle(BOSS_HOLE_D / 2)
        .extrude(BOSS_HOLE_DEPTH)
        .translate((hx, hy, Z_TOP_FEAT - BOSS_HOLE_DEPTH))
    )
    body = body.cut(hole)

# cross bridge: plate + two end legs standing on the floor
XB = XI - BAR_GAP
bar = block(-XB, XB, -BAR_T / 2, BAR_T / 2, BAR_Z0, BAR_Z1)
for sx in (-1, 1):
    leg = block(sx * XB, sx * (XB - LEG_W), -BAR_T / 2, BAR_T / 2,
                T_FLOOR - 0.01, BAR_Z0 + 0.01)
    bar = bar.union(leg)
body = body.union(bar)

# back pads
for px in (-PAD_X, PAD_X):
    for pz in (PAD_Z_OFF, H - PAD_Z_OFF):
        pad = (
            cq.Workplane("XZ", origin=(px, D / 2, pz))
            .circle(PAD_D / 2)
            .extrude(-PAD_H)
        )
        body = body.union(pad)

result = body.clean()

VIEW = {"azimuth": 45, "elevation": 26}
